import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (everything scales with the wheel/disc diameter D)
# ---------------------------------------------------------------------------
D = 100.0                      # disc diameter
U = D                          # unit for the proportional values below

# disc
DISC_R = 0.5 * U
DISC_T = 0.204 * U             # thickness along Y
DISC_CHAMFER = 0.033 * U       # chamfer on the back edge

# body (lever) -- origin at the centre of the round end, Z=0 on the disc axis
R_END = 0.385 * U              # radius of the round end of the lever
Z_BOT = -0.112 * U             # underside of lever and arm
Z_TOP = 0.154 * U              # top face of the lever
Z_ARM = 0.111 * U              # top face of the arm
CH_H = 0.060 * U               # lever top chamfer, horizontal
CH_V = 0.046 * U               # lever top chamfer, vertical

# disc position relative to round end centre
DISC_X = 0.839 * U
DISC_BACK_Y = -0.693 * U

# arm (rectangular bar joining lever and disc)
ARM_W = 0.870 * U              # width along X (centred on disc)
ARM_BACK_Y = -0.409 * U        # arm end (towards +Y)
ARM_EDGE_FILLET = 0.022 * U      # rounded long edges of the arm
WEB_A = (0.777 * U, -0.565 * U)  # diagonal split line on the arm top
WEB_STEP = 0.003 * U

# lever flank curves (concave arcs tangent to the round end, convex arc to the tip)
UP_R = 2.46 * U                # upper flank radius
UP_ANG = 36.4                  # tangency angle on the round end (deg)
LO_R = 0.705 * U               # lower flank radius
LO_ANG = 263.0                 # tangency angle (deg)
CV_R = 0.743 * U               # convex arc from the lower corner to the tip

# dome (knob) on the round end
DOME_R0 = 0.274 * U
DOME_BAND = 0.016 * U
DOME_R1 = 0.188 * U
DOME_H = 0.122 * U
N_SCALLOP = 12
SCALLOP_RC = 0.275 * U
SCALLOP_R = 0.047 * U
PIN_RC = 0.261 * U
PIN_R = 0.016 * U
PIN_H = 0.020 * U
PIN_HOLE_R = 0.0105 * U
TOPDISC_R = 0.137 * U
TOPDISC_H = 0.013 * U
POCKET_RI = 0.075 * U
POCKET_RO = 0.131 * U
POCKET_HALF_ANG = 27.0
POCKET_D = 0.006 * U
BOSS_R0 = 0.056 * U
BOSS_R1 = 0.037 * U
BOSS_H = 0.016 * U
BORE_R = 0.087 * U
BORE_DEPTH = 0.16 * U

# square post + small hole on the lever
POST_X = 0.716 * U
POST_Y = -0.408 * U
POST_WX = 0.149 * U
POST_WY = 0.143 * U
POST_TOP = 0.326 * U
POST_WY_CORNER = 0.122 * U     # Y width at the corners (Y faces bulge)
POST_FILLET = 0.020 * U
POST_TOP_CHAMFER = 0.014 * U
POST_RECESS_R = 0.100 * U
POST_RECESS_D = 0.010 * U
HOLE_X = 0.492 * U
HOLE_Y = -0.409 * U
HOLE_R = 0.020 * U
HOLE_CSK_R = 0.039 * U          # 90 deg countersink outer radius


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def pol(r, a_deg, c=(0.0, 0.0)):
    a = math.radians(a_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def arc_mid(c, r, p0, p1, ccw):
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    if ccw:
        while a1 <= a0:
            a1 += 2 * math.pi
    else:
        while a1 >= a0:
            a1 -= 2 * math.pi
    am = 0.5 * (a0 + a1)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


# ---------------------------------------------------------------------------
# lever outline
# ---------------------------------------------------------------------------
arm_x0 = DISC_X - ARM_W / 2
arm_x1 = DISC_X + ARM_W / 2

Pu = pol(R_END, UP_ANG)
Cu = pol(R_END + UP_R, UP_ANG)
Pl = pol(R_END, LO_ANG)
Cl = pol(R_END + LO_R, LO_ANG)

# tip T : upper flank meets the arm end line
T = (Cu[0] - math.sqrt(UP_R ** 2 - (ARM_BACK_Y - Cu[1]) ** 2), ARM_BACK_Y)
# lower corner L : lower flank meets the arm side line
L = (arm_x0, Cl[1] + math.sqrt(LO_R ** 2 - (arm_x0 - Cl[0]) ** 2))

# convex arc centre (towards the lever interior)
mx, my = (L[0] + T[0]) / 2, (L[1] + T[1]) / 2
dx, dy = T[0] - L[0], T[1] - L[1]
chord = math.hypot(dx, dy)
h = math.sqrt(CV_R ** 2 - (chord / 2) ** 2)
nx, ny = -dy / chord, dx / chord          # left normal of L->T
Cv = (mx + nx * h, my + ny * h)


def circ_int(c0, r0, c1, r1, near):
    dx, dy = c1[0] - c0[0], c1[1] - c0[1]
    d = math.hypot(dx, dy)
    a = (r0 * r0 - r1 * r1 + d * d) / (2 * d)
    hh = math.sqrt(max(r0 * r0 - a * a, 0.0))
    xm, ym = c0[0] + a * dx / d, c0[1] + a * dy / d
    p1 = (xm + hh * dy / d, ym - hh * dx / d)
    p2 = (xm - hh * dy / d, ym + hh * dx / d)
    d1 = math.hypot(p1[0] - near[0], p1[1] - near[1])
    d2 = math.hypot(p2[0] - near[0], p2[1] - near[1])
    return p1 if d1 < d2 else p2


def lever_wire(off, z):
    """outline of the lever, offset inwards by 'off', at height z"""
    r_end = R_END - off
    r_up = UP_R + off
    r_lo = LO_R + off
    r_cv = CV_R - off
    pu = pol(r_end, UP_ANG)
    pl = pol(r_end, LO_ANG)
    t = circ_int(Cu, r_up, Cv, r_cv, T)
    l_ = circ_int(Cl, r_lo, Cv, r_cv, L)
    w = (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(*pu)
        .threePointArc(pol(r_end, 0.5 * (UP_ANG + LO_ANG)), pl)
        .threePointArc(arc_mid(Cl, r_lo, pl, l_, False), l_)
        .threePointArc(arc_mid(Cv, r_cv, l_, t, True), t)
        .threePointArc(arc_mid(Cu, r_up, t, pu, False), pu)
        .close()
    )
    return w


lever_base = lever_wire(0.0, Z_BOT).extrude(Z_TOP - CH_V - Z_BOT)
w_lo = lever_wire(0.0, Z_TOP - CH_V).ctx.pendingWires[0]
w_hi = lever_wire(CH_H, Z_TOP).ctx.pendingWires[0]
lever_top = cq.Solid.makeLoft([w_lo, w_hi], True)
lever = lever_base.union(cq.Workplane().add(lever_top))

# ---------------------------------------------------------------------------
# arm
# ---------------------------------------------------------------------------
arm = (
    cq.Workplane("XY")
    .box(ARM_W, ARM_BACK_Y - DISC_BACK_Y + 0.02 * U, Z_ARM - Z_BOT, centered=False)
    .translate((arm_x0, DISC_BACK_Y - 0.02 * U, Z_BOT))
)
arm_sel = cq.selectors.BoxSelector(
    (arm_x1 - 0.05 * U, DISC_BACK_Y + 0.01 * U, Z_BOT - 0.01 * U),
    (arm_x1 + 0.05 * U, ARM_BACK_Y + 0.05 * U, Z_ARM + 0.01 * U))
arm_edges = arm.edges(arm_sel).edges("|Y").vals() + arm.faces(">Y").edges("|X").vals()
arm = arm.newObject(arm_edges).fillet(ARM_EDGE_FILLET)

body = lever.union(arm)

# shallow relief on the arm top between the lever and the disc (diagonal edge)
relief = (
    cq.Workplane("XY", origin=(0, 0, Z_ARM - WEB_STEP))
    .polyline([WEB_A, (arm_x1 + 0.01 * U, DISC_BACK_Y), (arm_x0 - 0.01 * U, DISC_BACK_Y),
               (arm_x0 - 0.01 * U, L[1] + 0.05 * U), (WEB_A[0] - 0.05 * U, WEB_A[1] + 0.05 * U)])
    .close()
    .extrude(WEB_STEP + 0.01 * U)
)
relief = relief.cut(lever)
body = body.cut(relief)

# ---------------------------------------------------------------------------
# disc
# ---------------------------------------------------------------------------
# seam of the rim placed on the lower back side where it is out of sight
SEAM_A = math.radians(35.0)
disc_plane = cq.Plane(origin=(DISC_X, DISC_BACK_Y, 0),
                      xDir=(-math.sin(SEAM_A), 0, -math.cos(SEAM_A)), normal=(0, -1, 0))
disc = cq.Workplane(disc_plane).circle(DISC_R).extrude(DISC_T)   # towards -Y
disc = disc.faces(">Y").edges().chamfer(DISC_CHAMFER)
body = body.union(disc)

# ---------------------------------------------------------------------------
# dome / knob
# ---------------------------------------------------------------------------
z0 = Z_TOP
dome = (
    cq.Workplane("XZ", origin=(0, 0, 0))
    .moveTo(0, z0)
    .lineTo(DOME_R0, z0)
    .lineTo(DOME_R0, z0 + DOME_BAND)
    .lineTo(DOME_R1, z0 + DOME_H)
    .lineTo(0, z0 + DOME_H)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
# scallops
for i in range(N_SCALLOP):
    a = 360.0 * i / N_SCALLOP
    x, y = pol(SCALLOP_RC, a)
    cutter = (
        cq.Workplane("XY", origin=(x, y, z0))
        .circle(SCALLOP_R)
        .extrude(DOME_H + 0.01 * U)
    )
    dome = dome.cut(cutter)

# raised top disc with four sector pockets
ztop = z0 + DOME_H
topdisc = cq.Workplane("XY", origin=(0, 0, ztop)).circle(TOPDISC_R).extrude(TOPDISC_H)
for k in range(4):
    ac = 45.0 + 90.0 * k
    a0, a1 = ac - POCKET_HALF_ANG, ac + POCKET_HALF_ANG
    p_in0 = pol(POCKET_RI, a0)
    p_out0 = pol(POCKET_RO, a0)
    p_out1 = pol(POCKET_RO, a1)
    p_in1 = pol(POCKET_RI, a1)
    pocket = (
        cq.Workplane("XY", origin=(0, 0, ztop + TOPDISC_H - POCKET_D))
        .moveTo(*p_in0)
        .lineTo(*p_out0)
        .threePointArc(pol(POCKET_RO, ac), p_out1)
        .lineTo(*p_in1)
        .threePointArc(pol(POCKET_RI, ac), p_in0)
        .close()
        .extrude(TOPDISC_H + 0.01 * U)
    )
    topdisc = topdisc.cut(pocket)
dome = dome.union(topdisc)

# central boss (flared foot, flat top)
zb = ztop + TOPDISC_H
boss = (
    cq.Workplane("XZ")
    .moveTo(0, zb - 0.002 * U)
    .lineTo(BOSS_R0, zb - 0.002 * U)
    .lineTo(BOSS_R0, zb)
    .threePointArc(
        (BOSS_R1 + 0.29 * (BOSS_R0 - BOSS_R1), zb + 0.29 * BOSS_H * 0.8),
        (BOSS_R1, zb + 0.8 * BOSS_H),
    )
    .lineTo(BOSS_R1, zb + BOSS_H)
    .lineTo(0, zb + BOSS_H)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
dome = dome.union(boss)

# pins at the foot of each scallop
for i in range(N_SCALLOP):
    a = 360.0 * i / N_SCALLOP
    x, y = pol(PIN_RC, a)
    pin = (
        cq.Workplane("XY", origin=(x, y, z0 - 0.002 * U))
        .circle(PIN_R)
        .extrude(PIN_H + 0.002 * U)
        .faces(">Z").workplane().hole(2 * PIN_HOLE_R, PIN_H * 0.8)
    )
    dome = dome.union(pin)

body = body.union(dome)

# ---------------------------------------------------------------------------
# square post with a round recess, small countersunk hole
# ---------------------------------------------------------------------------
recess = (
    cq.Workplane("XY", origin=(POST_X, POST_Y, Z_TOP - POST_RECESS_D))
    .circle(POST_RECESS_R)
    .extrude(POST_RECESS_D + 0.01 * U)
)
body = body.cut(recess)
z_post0 = Z_TOP - POST_RECESS_D - 0.002 * U
hx, hy0, hy1 = POST_WX / 2, POST_WY_CORNER / 2, POST_WY / 2
post_sk = (
    cq.Sketch()
    .arc((-hx, -hy0), (0, -hy1), (hx, -hy0))
    .segment((hx, -hy0), (hx, hy0))
    .arc((hx, hy0), (0, hy1), (-hx, hy0))
    .segment((-hx, hy0), (-hx, -hy0))
    .assemble()
    .vertices()
    .fillet(POST_FILLET)
)
post = (
    cq.Workplane("XY", origin=(POST_X, POST_Y, z_post0))
    .placeSketch(post_sk)
    .extrude(POST_TOP - POST_TOP_CHAMFER - z_post0)
)
# chamfered top: ruled loft from the outline to its inward offset
pw0 = post.faces(">Z").wires().val()
pw1 = pw0.offset2D(-POST_TOP_CHAMFER, "arc")[0].moved(cq.Location(cq.Vector(0, 0, POST_TOP_CHAMFER)))
post = post.union(cq.Workplane().add(cq.Solid.makeLoft([pw0, pw1], True)))
body = body.union(post)

hole_cut = (
    cq.Workplane("XY", origin=(HOLE_X, HOLE_Y, Z_TOP - 0.06 * U))
    .circle(HOLE_R)
    .extrude(0.07 * U)
)
csk_h = HOLE_CSK_R - HOLE_R
csk = cq.Solid.makeCone(HOLE_R, HOLE_CSK_R + 0.001 * U, csk_h + 0.001 * U,
                        pnt=cq.Vector(HOLE_X, HOLE_Y, Z_TOP - csk_h))
body = body.cut(hole_cut).cut(cq.Workplane().add(csk))

# ---------------------------------------------------------------------------
# blind bore from below, concentric with the knob
# ---------------------------------------------------------------------------
bore = cq.Workplane("XY", origin=(0, 0, Z_BOT - 0.01 * U)).circle(BORE_R).extrude(BORE_DEPTH + 0.01 * U)
body = body.cut(bore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
